import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
R_RIM = 120.0          # outer radius of the rim
H_TOTAL = 27.5         # overall height (bottom of foot to top of rim)
FOOT_H = 3.0           # height of the solid foot disc under the plate
FOOT_FLARE = 0.5       # foot disc is this much wider at its bottom than at the wall
WALL_ANGLE = 42.6      # straight wall inclination from horizontal (deg)
KNEE_R = 25.0          # convex blend radius between wall and flange
FLANGE_R = 99.3        # concave radius of the flaring flange
FLANGE_MIN_ANGLE = 22.0  # flattest flange slope, where knee blend meets flange (deg)
RIM_ANGLE = 32.0       # flange slope right at the rim (deg)
BASE_SHIFT_Y = -1.0    # the base / wall bottom sits slightly off the rim axis (-Y)
T = 0.5                # sheet thickness

# ---------------- derived profile (outer skin, r-z plane) ----------------
aw = math.radians(WALL_ANGLE)
a1 = math.radians(FLANGE_MIN_ANGLE)
ar = math.radians(RIM_ANGLE)


def _add(p, q, s=1.0):
    return (p[0] + s * q[0], p[1] + s * q[1])


def _dn(a):
    """unit vector pointing down/outward, normal to a profile of slope a"""
    return (math.sin(a), -math.cos(a))


def _up(a):
    """unit vector pointing up/inward (into the bowl), normal to slope a"""
    return (-math.sin(a), math.cos(a))


E = (R_RIM, H_TOTAL)                           # rim point
CF = _add(E, _up(ar), FLANGE_R)                # flange arc centre (above)
P1 = _add(CF, _dn(a1), FLANGE_R)               # knee / flange junction
CK = _add(P1, _dn(a1), KNEE_R)                 # knee arc centre (below)
W = _add(CK, _dn(aw), -KNEE_R)                 # wall / knee junction
R_WALL_BOT = W[0] - (W[1] - FOOT_H) / math.tan(aw)

am_f = 0.5 * (a1 + ar)
am_k = 0.5 * (a1 + aw)
MF = _add(CF, _dn(am_f), FLANGE_R)             # flange arc midpoint
MK = _add(CK, _dn(am_k), -KNEE_R)              # knee arc midpoint


def profile_solid(off):
    """Filled body bounded by the plate skin offset inward by `off`.

    off = 0 is the outer skin; off = T is the inner skin, continued above the rim
    so that subtracting it leaves an open-topped sheet of thickness T."""
    w = _add(W, _up(aw), off)
    mk = _add(MK, _up(am_k), off)
    p1 = _add(P1, _up(a1), off)
    mf = _add(MF, _up(am_f), off)
    e = _add(E, _up(ar), off)

    # straight, slightly skewed conical wall: ruled loft bottom circle -> knee start
    z_bot = FOOT_H + off
    r_bot = w[0] - (w[1] - z_bot) / math.tan(aw)
    c_bot = cq.Wire.makeCircle(r_bot, cq.Vector(0, BASE_SHIFT_Y, z_bot), cq.Vector(0, 0, 1))
    c_top = cq.Wire.makeCircle(w[0], cq.Vector(0, 0, w[1]), cq.Vector(0, 0, 1))
    wall = cq.Workplane("XY").add(cq.Solid.makeLoft([c_bot, c_top], True))

    # knee blend + flaring flange, revolved about the plate axis
    wp = (
        cq.Workplane("XZ")
        .moveTo(0.0, w[1])
        .lineTo(w[0], w[1])
        .threePointArc(mk, p1)
        .threePointArc(mf, e)
    )
    if off == 0:
        z_cap = H_TOTAL
    else:
        z_cap = H_TOTAL + 5.0
        wp = wp.lineTo(e[0] + (z_cap - e[1]) / math.tan(ar), z_cap)
    upper = wp.lineTo(0.0, z_cap).close().revolve(360.0, (0, 0, 0), (0, 1, 0))
    return wall.union(upper, clean=True)


outer = profile_solid(0.0)
inner = profile_solid(T)
plate = outer.cut(inner)

# solid foot disc under the flat bottom, flaring very slightly towards the table
foot_top = FOOT_H + T * 0.5
foot = (
    cq.Workplane("XZ", origin=(0, BASE_SHIFT_Y, 0))
    .polyline([
        (0.0, 0.0),
        (R_WALL_BOT + FOOT_FLARE, 0.0),
        (R_WALL_BOT - 0.05, FOOT_H),
        (R_WALL_BOT - 0.05, foot_top),
        (0.0, foot_top),
    ])
    .close()
    .revolve(360.0, (0, 0, 0), (0, 1, 0))
)

result = plate.union(foot)

VIEW = {"azimuth": 45, "elevation": 26}
